import math
import cadquery as cq

# ---------------------------------------------------------------
# Outboard-style lower unit: mounting pad + anti-ventilation plate,
# streamlined strut, torpedo gear housing and skeg.
# Coordinates: Y = 0 at the pad front tip, +Y toward the wide plate,
# Z = 0 at the pad top face, part hangs downward (-Z).
# ---------------------------------------------------------------

# ---- mounting pad ----
PAD_T = 15.4          # pad thickness
PAD_HW = 40.7         # max half width of the pad
PAD_BACK = 148.0      # Y of pad back edge
PAD_BACK_R = 14.0     # back corner radius
PAD_SIDE_END = 126.0  # where the curved front outline becomes straight
PAD_DRAFT = 10.5      # side-wall draft (deg)
UNDER_KEEL_HW = 22.5  # flat keel band half width on the underside
UNDER_VEE_SLOPE = 0.12  # underside rises outward with this slope
# half-width of the pad outline at given Y (front outline, spline through these)
PAD_OUTLINE = [(40.1, 110.0), (38.5, 82.0), (35.7, 54.0), (33.7, 40.4), (30.2, 25.5),
               (23.7, 11.5), (13.1, 3.0)]

# ---- anti-ventilation plate ----
PL_FRONT = 60.0       # plate starts (hidden inside the pad)
PL_HW_FRONT = 31.7    # half width at PL_FRONT (planform)
PL_BACK = 233.6       # Y of back corners
PL_BACK_C = 236.35     # Y of back edge at centre (slightly convex)
PL_HW_BACK = 67.4     # half width at back corners (before rounding)
PL_CORNER_R = 6.0
PL_SEC_W = 72.0       # half width of the loft sections (trimmed by planform)
PL_TOP_C = -0.15      # plate crown height at the pad back edge
PL_BOT_C = -15.0      # plate keel height at the pad back edge
PL_MID_DROP = 7.24    # crown drop of the top at x=+-72 (pad back section)
PL_MID_RISE = 4.9     # rise of the underside at x=+-72 (pad back section)
PL_S0_DROP = -6.31
PL_S0_RISE = -1.84
PL_BACK_DROP = -0.39
PL_BACK_RISE = -1.84
PL_T_BACK_TOP = -5.9  # centre top height of the far loft section
PL_T_BACK_BOT = -9.49 # centre bottom height of the far loft section

# ---- strut (z, Y leading edge, Y trailing edge, half thickness) ----
STRUT_TOP = (-8.0, 41.0, 140.6, 19.4)
STRUT_MID = (-42.0, 46.7, 139.0, 16.5)
STRUT_BOT = (-90.0, 53.5, 135.9, 14.2)
STRUT_TOP_FILLET = 3.0
FOIL_SMAX = 0.30      # position of max thickness (fraction of chord)
FOIL_TAPER_EXP = 3.0  # taper exponent toward the trailing edge
STRUT_TORP_FILLET = 10.0

# ---- torpedo ----
TORP_Z = -91.0
TORP_R = 15.35
TORP_NOSE_Y = 38.9
TORP_NOSE_R = 10.3     # radius where the conical nose starts
NOSE_CHAMFER = 1.0
TORP_CONE_SLOPE = 0.117
TORP_CONE_END = 76.0   # straight cone ends here ...
TORP_FULL_Y = 90.0     # ... and blends into the cylinder here
TORP_TAIL_Y = 147.0
TORP_TAIL_FILLET = 2.5
NOSE_BORE_D = 15.4
TAIL_BORE_D = 24.5

# ---- skeg (z, Y leading edge, Y trailing edge, half thickness) ----
SKEG_TOP = (-100.0, 74.5, 135.3, 6.8)
SKEG_BOT = (-144.8, 108.2, 135.3, 2.3)
SKEG_FILLET = 6.0

# ---- holes on pad ----
TIP_HOLE = (0.0, 15.7, 11.5)
FRONT_PAIR = (19.0, 50.2, 8.0)
BACK_PAIR = (24.2, 132.1, 8.0)
UNDER_CBORE_D = 14.0  # counterbore (from below) of the rear bolt holes
UNDER_CBORE_H = 5.0
CSK = (0.0, 65.4, 18.7, 16.2, 1.25, 5.0, 11.0)  # x, y, top D, step d, csk depth, step depth, hole d
CBORE = (0.0, 102.4, 18.6, 37.4, 4.5, 2.0)      # x, y, bore d, cbore D, cbore depth, chamfer


def foil_wire(z, y_le, y_te, t, te=1.0, s_max=FOIL_SMAX, p=FOIL_TAPER_EXP):
    """Symmetric streamlined section in a horizontal plane at height z:
    elliptical nose up to s_max of the chord, then a power-law taper to a
    small rounded trailing edge.  One smooth periodic spline."""
    c = y_te - y_le

    def half_t(s):
        if s <= s_max:
            u = (s_max - s) / s_max
            return t * math.sqrt(max(1.0 - u * u, 0.0))
        u = (s - s_max) / (1.0 - s_max)
        return te + (t - te) * (1.0 - u ** p)

    ss = [0.97, 0.85, 0.7, 0.5, 0.3, 0.15, 0.06, 0.015]
    half = [(max(half_t(s), te), y_le + s * c) for s in ss]
    pts = [cq.Vector(0.0, y_te, z)]
    pts += [cq.Vector(x, y, z) for (x, y) in half]
    pts.append(cq.Vector(0.0, y_le, z))
    pts += [cq.Vector(-x, y, z) for (x, y) in reversed(half)]
    return cq.Wire.assembleEdges([cq.Edge.makeSpline(pts, periodic=True)])


def edges_between(shape, a, b, tol=1e-3):
    """Edges of `shape` lying on the surfaces of both solids a and b."""
    fa = cq.Compound.makeCompound(a.Faces())
    fb = cq.Compound.makeCompound(b.Faces())
    sel = []
    for e in shape.Edges():
        p = cq.Vertex.makeVertex(*e.positionAt(0.5).toTuple())
        if p.distance(fa) < tol and p.distance(fb) < tol:
            sel.append(e)
    return sel


def fuse_fillet(a, b, r):
    """Union of two solids with a fillet along their intersection."""
    u = a.fuse(b).clean()
    sel = edges_between(u, a, b)
    if sel:
        try:
            f = u.fillet(r, sel)
            if f.isValid():
                return f
        except Exception:
            pass
    return u


# ---------------- mounting pad ----------------
# outline: spline nose, straight sides, rounded back corners.  The side walls
# carry a draft: ruled loft from the top outline to the inset bottom outline.
def pad_wire(inset, z):
    hw = PAD_HW - inset
    r = PAD_BACK_R - inset
    back = PAD_BACK - inset
    c_y = PAD_BACK - PAD_BACK_R
    # outline points (left side down to the tip, then up the right side)
    pts = ([(-PAD_HW, PAD_SIDE_END)] + [(-x, y) for (x, y) in PAD_OUTLINE]
           + [(0.0, 0.0)] + [(x, y) for (x, y) in reversed(PAD_OUTLINE)]
           + [(PAD_HW, PAD_SIDE_END)])
    moved = []
    for i, (x, y) in enumerate(pts):
        if i == 0:
            tx, ty = 0.0, -1.0
        elif i == len(pts) - 1:
            tx, ty = 0.0, 1.0
        else:
            tx, ty = pts[i + 1][0] - pts[i - 1][0], pts[i + 1][1] - pts[i - 1][1]
        n = math.hypot(tx, ty)
        nx, ny = ty / n, -tx / n           # outward normal (CCW outline)
        moved.append((x - inset * nx, y - inset * ny))
    wp = (
        cq.Workplane("XY", origin=(0, 0, z))
        .moveTo(*moved[0])
        .spline(moved[1:], tangents=[(0, -1), (0, 1)], includeCurrent=True)
        .lineTo(hw, c_y)
        .radiusArc((hw - r, back), r)
        .lineTo(-(hw - r), back)
        .radiusArc((-hw, c_y), r)
        .close()
    )
    return wp.val()


pad_inset = PAD_T * math.tan(math.radians(PAD_DRAFT))
pad = cq.Workplane("XY").add(
    cq.Solid.makeLoft([pad_wire(0.0, 0.0), pad_wire(pad_inset, -PAD_T)], True))

# ---------------- anti-ventilation plate ----------------
def plate_section(y, zt, dt, zb, db, w=PL_SEC_W):
    """Crowned plate cross-section (XZ plane at Y=y): top arc through the
    centre height zt dropping by dt at +-w, bottom arc through zb rising by db."""
    v = lambda x, z: cq.Vector(x, y, z)
    e = [
        cq.Edge.makeThreePointArc(v(-w, zt - dt), v(0, zt), v(w, zt - dt)),
        cq.Edge.makeLine(v(w, zt - dt), v(w, zb + db)),
        cq.Edge.makeThreePointArc(v(w, zb + db), v(0, zb), v(-w, zb + db)),
        cq.Edge.makeLine(v(-w, zb + db), v(-w, zt - dt)),
    ]
    return cq.Wire.assembleEdges(e)


# three sections symmetric about the pad back edge so the smooth loft peaks
# exactly there (flush with the pad top) and falls away toward the trailing edge
PL_SPAN = PL_BACK_C + 6.0 - PAD_BACK
s0 = plate_section(PAD_BACK - PL_SPAN, PL_T_BACK_TOP, PL_S0_DROP,
                   PL_T_BACK_BOT, PL_S0_RISE)
s1 = plate_section(PAD_BACK, PL_TOP_C, PL_MID_DROP, PL_BOT_C, PL_MID_RISE)
s2 = plate_section(PAD_BACK + PL_SPAN, PL_T_BACK_TOP, PL_BACK_DROP,
                   PL_T_BACK_BOT, PL_BACK_RISE)
plate_loft = cq.Solid.makeLoft([s0, s1, s2], False)

# plan outline of the plate at the level of its top face (z = PL_REF_Z); its
# side walls carry the same draft as the pad walls so they emerge cleanly
PL_REF_Z = -6.0


def plate_outline(offset, z):
    w = (
        cq.Workplane("XY", origin=(0, 0, z))
        .moveTo(-PL_HW_FRONT, PL_FRONT)
        .lineTo(PL_HW_FRONT, PL_FRONT)
        .lineTo(PL_HW_BACK, PL_BACK)
        .threePointArc((0, PL_BACK_C), (-PL_HW_BACK, PL_BACK))
        .close()
        .extrude(1)
        .edges("|Z").edges(">Y").fillet(PL_CORNER_R)
        .faces("<Z").wires().val()
    )
    return w.offset2D(offset, "arc")[0] if abs(offset) > 1e-9 else w


tan_d = math.tan(math.radians(PAD_DRAFT))
planform = cq.Solid.makeLoft(
    [plate_outline((5.0 - PL_REF_Z) * tan_d, 5.0),
     plate_outline(-(PL_REF_Z + 20.0) * tan_d, -20.0)], True)
plate = cq.Workplane("XY").add(plate_loft).intersect(planform)

# ---------------- strut ----------------
strut = cq.Solid.makeLoft(
    [foil_wire(*STRUT_TOP), foil_wire(*STRUT_MID), foil_wire(*STRUT_BOT)], False)

# ---------------- torpedo ----------------
# revolved profile: flat chamfered nose face, conical nose blending into the
# cylindrical housing, rounded tail face
prof = (
    cq.Workplane("YZ")
    .moveTo(TORP_NOSE_Y, TORP_Z)
    .lineTo(TORP_NOSE_Y, TORP_Z + TORP_NOSE_R - NOSE_CHAMFER)
    .lineTo(TORP_NOSE_Y + NOSE_CHAMFER, TORP_Z + TORP_NOSE_R)
    .lineTo(TORP_CONE_END,
            TORP_Z + TORP_NOSE_R + TORP_CONE_SLOPE * (TORP_CONE_END - TORP_NOSE_Y - NOSE_CHAMFER))
    .spline([(TORP_FULL_Y, TORP_Z + TORP_R)],
            tangents=[(1, TORP_CONE_SLOPE), (1, 0)], includeCurrent=True)
    .lineTo(TORP_TAIL_Y - TORP_TAIL_FILLET, TORP_Z + TORP_R)
    .radiusArc((TORP_TAIL_Y, TORP_Z + TORP_R - TORP_TAIL_FILLET), TORP_TAIL_FILLET)
    .lineTo(TORP_TAIL_Y, TORP_Z)
    .close()
)
torpedo = prof.revolve(360, (0, TORP_Z, 0), (1, TORP_Z, 0)).val()

# ---------------- skeg ----------------
skeg = cq.Solid.makeLoft([foil_wire(*SKEG_TOP, te=2.0),
                          foil_wire(*SKEG_BOT, te=1.2)], True)

# ---------------- combine ----------------
lower = fuse_fillet(torpedo, skeg, SKEG_FILLET)
lower = fuse_fillet(lower, strut, STRUT_TORP_FILLET)

top_part = pad.union(plate).val()
body = fuse_fillet(top_part, lower, STRUT_TOP_FILLET)

# shallow vee on the underside of pad and plate: flat keel band around the
# strut, rising toward the edges
for side in (1, -1):
    vcut = (
        cq.Workplane("XY")
        .box(200, 400, 100, centered=(False, True, False))
        .translate((0, 120, -100))
        .rotate((0, 0, 0), (0, 1, 0), -math.degrees(math.atan(UNDER_VEE_SLOPE)))
        .translate((UNDER_KEEL_HW, 0, -PAD_T))
    )
    if side < 0:
        vcut = vcut.mirror("YZ")
    body = body.cut(vcut.val())
body = cq.Workplane("XY").add(body)

# ---------------- holes ----------------
top = cq.Workplane("XY")
body = body.cut(
    top.pushPoints([(TIP_HOLE[0], TIP_HOLE[1])]).circle(TIP_HOLE[2] / 2).extrude(-40)
)
small_pts = [(FRONT_PAIR[0], FRONT_PAIR[1]), (-FRONT_PAIR[0], FRONT_PAIR[1]),
             (BACK_PAIR[0], BACK_PAIR[1]), (-BACK_PAIR[0], BACK_PAIR[1])]
body = body.cut(top.pushPoints(small_pts).circle(FRONT_PAIR[2] / 2).extrude(-40))
# counterbores from the underside for the nuts of the rear bolt pair
body = body.cut(
    cq.Workplane("XY", origin=(0, 0, -PAD_T - 5.0)).pushPoints(small_pts[2:])
    .circle(UNDER_CBORE_D / 2).extrude(5.0 + UNDER_CBORE_H)
)
# countersunk stepped hole
cx, cy, cD, cd, ch_d, st_d, h_d = CSK
csk_tool = (
    cq.Workplane("XZ")
    .moveTo(0, 1)
    .lineTo(cD / 2, 1)
    .lineTo(cD / 2, 0)
    .lineTo(cd / 2, -ch_d)
    .lineTo(cd / 2, -st_d)
    .lineTo(h_d / 2, -st_d - (cd - h_d) / 2 * math.tan(math.radians(31)))
    .lineTo(h_d / 2, -30)
    .lineTo(0, -30)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((cx, cy, 0))
)
body = body.cut(csk_tool)
# counterbore with chamfered bore (drive-shaft bore)
bx, by, cb_d, cb_D, cb_h, ch = CBORE
cb_tool = (
    cq.Workplane("XZ")
    .moveTo(0, 1)
    .lineTo(cb_D / 2, 1)
    .lineTo(cb_D / 2, -cb_h)
    .lineTo(cb_d / 2 + ch, -cb_h)
    .lineTo(cb_d / 2, -cb_h - ch)
    .lineTo(cb_d / 2, -45)
    .lineTo(0, -45)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .translate((bx, by, 0))
)
body = body.cut(cb_tool)

# torpedo bores (prop-shaft exit at the nose, threaded bore at the tail)
nose_bore = (cq.Workplane("XZ", origin=(0, TORP_NOSE_Y, TORP_Z))
             .circle(NOSE_BORE_D / 2).extrude(-20))
tail_bore = (cq.Workplane("XZ", origin=(0, TORP_TAIL_Y, TORP_Z))
             .circle(TAIL_BORE_D / 2).extrude(26))
body = body.cut(nose_bore).cut(tail_bore)

result = body
